import math
import cadquery as cq

# ---------------------------------------------------------------
# Stool kit: four splayed sabre legs with slotted D-tenons,
# two small wedged feet blocks and a saddle block with a capped tenon.
# Units: mm.  Z up, all pieces stand on the XY plane.
# ---------------------------------------------------------------

# ---------------- legs (canonical leg = front-left, -X/-Y) -------
LEG_MIRROR_X = -53.6           # legs are mirrored about X = LEG_MIRROR_X and Y = 0
TOP_Z = 179.0                  # shoulder height
# horizontal sections of the sabre leg: (z, xmin, xmax, ymin, ymax);
# straight in X, outer (-Y) face kicks out to a near-vertical foot
LEG_SECTIONS = [
    (0.0,   -119.0, -80.0, -95.5, -60.0),
    (40.0,  -114.3, -77.3, -92.2, -55.8),
    (100.0, -107.3, -73.35, -81.5, -48.2),
    (150.0, -101.5, -70.0, -71.0, -41.2),
]
TOP_C = (-83.1, -51.0)         # shoulder centre (section normal to the axis)
TOP_W, TOP_D = 30.0, 27.8      # shoulder section size
LEG_TOP_SLOPE = (0.092, 0.175) # dX/dZ, dY/dZ of the axis at the shoulder
LEG_R = 5.0                    # rounding of the four long edges
FOOT_FILLET = 2.5

TEN_H = 38.5                   # tenon height along axis
TEN_RB, TEN_RT = 12.6, 10.4    # D-tenon half size at base / top
TEN_SLOT_W = 4.8
TEN_INNER = 0.9                # depth of the square inner block / radius
TEN_BLOCK_W = 0.84             # half width of the inner block / radius
TEN_SLOT_D = 36.5              # slot depth from tenon top

# ---------------- small wedge blocks ---------------------------
SB_BASE_X = (36.0, 77.5)
SB_BASE_Y = (-89.0, -63.5)     # outer face nearly vertical, inner face sloped
SB_TOP_X = (43.5, 71.0)
SB_TOP_Y = (-90.0, -75.8)
SB_TOP_Z = 63.0
SB_CAPB_X = (41.5, 71.9)       # cap bottom (overhangs the body = ledge)
SB_CAPB_Y = (-91.6, -75.0)
SB_CAPT_X = (44.2, 70.6)       # cap top (cap keeps tapering)
SB_CAPT_Y = (-91.3, -78.5)
SB_CAP_Z = 82.5
SB_CAP_R = 2.5
SB_SLOT_X = 57.2
SB_SLOT_W = 4.5
SB_SLOT_Z = 52.5
SB2_DY = 3.0                   # the +Y block sits slightly further out

# ---------------- saddle block ---------------------------------
CB_BOT_X = (78.0, 115.5)
CB_BOT_Y = (-25.5, 26.5)
CB_TOP_X = (65.8, 119.2)
CB_TOP_Y = (-38.5, 41.0)
CB_H = 92.0
CB_R = 4.0                      # vertical corner radius
SAD_R = 80.0                   # saddle cylinder radius
SAD_B1 = (67.0, 13.0, 69.0)    # lowest saddle line at the -X face
SAD_B2 = (118.0, 7.0, 53.0)    # lowest saddle line at the +X face
CT_FLAT = 84.5                 # flat side X of the D tenon (circle centre)
CT_R = 26.0                    # D tenon radius
CT_CLIP = 106.2                # second (clipping) flat on +X side
CT_SLOT_Y = 0.5
CT_TOP = 100.0                 # top of tenon body
CT_BASE_Z = 40.0               # tenon body starts inside the block
CT_LEAN = 3.0                  # flat face leans out by this much at CT_BASE_Z
CAP_H = 8.5
CT_SLOT_W = 5.5
CT_ROOT_R = 5.0                # blend between tenon and saddle
CT_SLOT_Z = 75.0


def safe_fillet(wp, edges, r):
    """Fillet the given edges; keep the unfilleted solid if the result is bad."""
    try:
        out = wp.newObject(edges).fillet(r)
        if out.val().isValid():
            return out
    except Exception:
        pass
    return wp


def unit(v):
    n = math.sqrt(sum(c * c for c in v))
    return tuple(c / n for c in v)


def make_leg():
    def quad(pl, w, d):
        return cq.Workplane(pl).rect(w, d).wires().val()

    wires = []
    for (z, x0, x1, y0, y1) in LEG_SECTIONS:
        pl = cq.Plane(origin=((x0 + x1) / 2, (y0 + y1) / 2, z), xDir=(1, 0, 0), normal=(0, 0, 1))
        wires.append(quad(pl, x1 - x0, y1 - y0))
    axis = unit((LEG_TOP_SLOPE[0], LEG_TOP_SLOPE[1], 1.0))
    xd = unit((1.0 - axis[0] * axis[0], -axis[0] * axis[1], -axis[0] * axis[2]))
    p_top = cq.Plane(origin=(TOP_C[0], TOP_C[1], TOP_Z), xDir=xd, normal=axis)
    wires.append(quad(p_top, TOP_W, TOP_D))

    body = cq.Workplane("XY").add(cq.Solid.makeLoft(wires, False))
    # round the four long edges, then soften the foot
    long_edges = [e for e in body.val().Edges()
                  if abs(e.startPoint().z - e.endPoint().z) > 0.5 * TOP_Z]
    body = safe_fillet(body, long_edges, LEG_R)
    body = safe_fillet(body, body.faces("<Z").edges().vals(), FOOT_FILLET)

    # D-shaped tapered tenon: square half toward the inside (+local y),
    # round half toward the outside, slot across the middle.
    def d_wire(pl, r):
        di = TEN_INNER * r          # depth of the square inner block
        wi = TEN_BLOCK_W * r        # half width of the inner block
        return (cq.Workplane(pl)
                .moveTo(-wi, 0).lineTo(-wi, di).lineTo(wi, di).lineTo(wi, 0)
                .lineTo(r, 0).threePointArc((0, -r), (-r, 0)).close().wires().val())

    p_tb = cq.Plane(origin=(0, 0, -1.0), xDir=(1, 0, 0), normal=(0, 0, 1))
    p_tt = cq.Plane(origin=(0, 0, TEN_H), xDir=(1, 0, 0), normal=(0, 0, 1))
    ten = cq.Workplane("XY").add(cq.Solid.makeLoft([d_wire(p_tb, TEN_RB), d_wire(p_tt, TEN_RT)], True))
    slot = (cq.Workplane("XY")
            .box(3 * TEN_RB, TEN_SLOT_W, TEN_SLOT_D + 5, centered=(True, True, False))
            .translate((0, 0, TEN_H - TEN_SLOT_D)))
    ten = ten.cut(slot)
    # place tenon in the shoulder frame
    loc = cq.Location(p_top)
    ten_shape = ten.val().moved(loc)
    leg = body.union(cq.Workplane("XY").add(ten_shape))
    return leg.val()


def make_small_block():
    def rect_wire(z, xr, yr):
        return (cq.Workplane("XY").workplane(offset=z)
                .center((xr[0] + xr[1]) / 2, (yr[0] + yr[1]) / 2)
                .rect(xr[1] - xr[0], yr[1] - yr[0]).wires().val())

    body = cq.Workplane("XY").add(cq.Solid.makeLoft(
        [rect_wire(0.0, SB_BASE_X, SB_BASE_Y), rect_wire(SB_TOP_Z + 0.5, SB_TOP_X, SB_TOP_Y)], True))
    cap = cq.Workplane("XY").add(cq.Solid.makeLoft(
        [rect_wire(SB_TOP_Z, SB_CAPB_X, SB_CAPB_Y), rect_wire(SB_CAP_Z, SB_CAPT_X, SB_CAPT_Y)], True))
    vert = [e for e in cap.val().Edges() if abs(e.startPoint().z - e.endPoint().z) > 1.0]
    cap = safe_fillet(cap, vert, SB_CAP_R)
    blk = body.union(cap)
    slot = (cq.Workplane("XY")
            .box(SB_SLOT_W, 60, SB_CAP_Z, centered=(True, True, False))
            .translate((SB_SLOT_X, (SB_BASE_Y[0] + SB_BASE_Y[1]) / 2, SB_SLOT_Z)))
    return blk.cut(slot).val()


def make_saddle_block():
    wb = (cq.Workplane("XY")
          .center((CB_BOT_X[0] + CB_BOT_X[1]) / 2, (CB_BOT_Y[0] + CB_BOT_Y[1]) / 2)
          .rect(CB_BOT_X[1] - CB_BOT_X[0], CB_BOT_Y[1] - CB_BOT_Y[0]).wires().val())
    wt = (cq.Workplane("XY").workplane(offset=CB_H)
          .center((CB_TOP_X[0] + CB_TOP_X[1]) / 2, (CB_TOP_Y[0] + CB_TOP_Y[1]) / 2)
          .rect(CB_TOP_X[1] - CB_TOP_X[0], CB_TOP_Y[1] - CB_TOP_Y[0]).wires().val())
    box = cq.Workplane("XY").add(cq.Solid.makeLoft([wb, wt], True))
    vert = [e for e in box.val().Edges() if abs(e.startPoint().z - e.endPoint().z) > 1.0]
    box = safe_fillet(box, vert, CB_R)

    # saddle: cylinder cut whose axis descends toward +X and drifts toward -Y
    b1 = cq.Vector(*SAD_B1)
    b2 = cq.Vector(*SAD_B2)
    d = (b2 - b1).normalized()
    down = (cq.Vector(0, 0, -1) + d * d.z).normalized()
    a1 = b1 - down * SAD_R
    cyl = cq.Solid.makeCylinder(SAD_R, 300, a1 - d * 120, d)
    blk = box.cut(cq.Workplane("XY").add(cyl))

    # D-shaped tenon: half disc centred on its flat (-X) side, clipped by a
    # second flat parallel to it on the +X side; tapered body plus cap.
    def seg_wire(z, cx, r, flat, clip):
        """Circle (centre cx, radius r) trimmed by X = flat and X = clip."""
        hf = math.sqrt(r * r - (flat - cx) ** 2)
        hc = math.sqrt(r * r - (clip - cx) ** 2)
        t1 = math.atan2(-hf, flat - cx)
        t2 = math.atan2(-hc, clip - cx)
        tm = (t1 + t2) / 2.0
        p1 = (cx + r * math.cos(tm), r * math.sin(tm))
        p2 = (p1[0], -p1[1])
        return (cq.Workplane("XY").workplane(offset=z)
                .moveTo(flat, -hf)
                .threePointArc(p1, (clip, -hc))
                .lineTo(clip, hc)
                .threePointArc(p2, (flat, hf))
                .close().wires().val())

    body = cq.Solid.makeLoft(
        [seg_wire(CT_BASE_Z, CT_FLAT - 1.0, CT_R + 2.0, CT_FLAT - CT_LEAN, CT_CLIP + 3.3),
         seg_wire(CT_TOP, CT_FLAT + 0.6, CT_R - 1.0, CT_FLAT + 0.6, CT_CLIP - 0.8)], True)
    cap = (cq.Workplane("XY").add(seg_wire(CT_TOP - 0.01, CT_FLAT, CT_R, CT_FLAT - 0.3, CT_CLIP))
           .toPending().extrude(CAP_H))
    cap = safe_fillet(cap, cap.faces(">Z").edges().vals(), 0.6)
    ten = cq.Workplane("XY").add(body).union(cap)
    # slot along X with rounded bottom
    sl = (cq.Workplane("YZ").workplane(offset=CT_FLAT - 10)
          .center(CT_SLOT_Y, (CT_SLOT_Z + CT_TOP + CAP_H + 5) / 2)
          .slot2D(CT_TOP + CAP_H + 5 - CT_SLOT_Z, CT_SLOT_W, angle=90)
          .extrude(CT_CLIP - CT_FLAT + 25))
    ten = ten.cut(sl)
    res = blk.union(ten)
    # blend the tenon into the saddle
    root = [e for e in res.val().Edges()
            if 76 < e.Center().x < 112 and abs(e.Center().y) < 32 and 45 < e.Center().z < 70]
    res = safe_fillet(res, root, CT_ROOT_R)
    return res.val()


# ---------------- assemble ----------------------------------
leg_c = make_leg()
leg_d = leg_c.mirror("YZ", (LEG_MIRROR_X, 0, 0))
leg_a = leg_c.mirror("XZ", (0, 0, 0))
leg_b = leg_d.mirror("XZ", (0, 0, 0))

sb1 = make_small_block()
sb2 = sb1.mirror("XZ", (0, 0, 0)).translate(cq.Vector(0, SB2_DY, 0))

cb = make_saddle_block()

result = cq.Workplane("XY").add(cq.Compound.makeCompound([leg_a, leg_b, leg_c, leg_d, sb1, sb2, cb]))
